import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 118.0          # overall length (Y)
W = 56.0           # overall width (X)
H_RIM = 31.5       # height of the open rim (side walls)
H_LID = 33.0       # height of the covered rear section (lid top)
FRONT_CURVE_LEN = 20.0   # length over which the side rim curves down to the front wall
FRONT_EY = 20.75         # semi-axis (Y) of the elliptical front drop
FRONT_EZ = 14.5          # semi-axis (Z) of the elliptical front drop
H_FRONT = H_RIM - FRONT_EZ + FRONT_EZ * math.sqrt(1.0 - (FRONT_CURVE_LEN / FRONT_EY) ** 2)  # front wall height
R_FRONT_CORNER = 6.5     # vertical corner radius, front
R_BACK_CORNER = 1.0      # vertical corner radius, back (outside)
R_BACK_INNER = 2.0       # vertical corner radius, back (inside)
R_BOTTOM = 1.0           # bottom edge rounding
RIM_ROUND = 0.6          # rounding of the rim top edges
T_WALL = 1.8             # wall thickness
T_FLOOR = 2.0            # floor thickness
LID_LEN = 28.0           # length of the rear lid (from back face)
LID_T = 1.5              # lid thickness
LID_CHAMFER = 1.5        # ramp in the side walls up to the lid
PLATFORM_H = 1.0         # raised floor under the lid
RIB_W = 1.3              # guide rib width (Y)
RIB_D = 1.0              # guide rib protrusion (X)
RIB_Y_FROM_LIDFRONT = (6.4, 19.9)

# front windows (x0, x1, z0, z1)
WINDOWS = [(-16.3, -4.1, 4.2, 15.5), (13.0, 22.3, 4.3, 15.3)]

# slotted screw bosses (x, y), slots run along Y
BOSS_W = 6.6
BOSS_LEN = 8.4
BOSS_H = 1.2
SLOT_W = 3.1
SLOT_LEN = 4.1
CSK_W = 6.6
CSK_LEN = 7.6
BOSSES = [(-7.4, 28.2), (22.0, -35.1)]

# embossed lettering
TEXT = "Mack"
TEXT_LEN = 68.0
TEXT_H = 21.6           # baseline to ascender
TEXT_YC = 2.3
TEXT_BASE_Z = 2.9
TEXT_H_LEFT = 22.8      # lettering on the -X side
TEXT_BASE_Z_LEFT = 3.3
TEXT_DEPTH = 0.8
FONT = "/usr/share/fonts/truetype/dejavu/DejaVuSerif-Bold.ttf"

# rear logo relief height
LOGO_DEPTH = 0.25

y_front = -L / 2.0
y_back = L / 2.0
y_lid = y_back - LID_LEN


# ---------------- helpers ----------------
def footprint(w, l, rf, rb, h, z0=0.0):
    """rounded-rectangle prism, big radius at the front (-Y), small at back"""
    b = cq.Workplane("XY").box(w, l, h, centered=(True, True, False)).translate((0, 0, z0))
    b = b.edges("|Z and <Y").fillet(rf)
    if rb > 0.05:
        b = b.edges("|Z and >Y").fillet(rb)
    return b


def side_profile():
    """YZ profile of the outer body (extruded across X): the side rim runs flat,
    then drops to the front wall along a quarter-ellipse"""
    cy = y_front + FRONT_CURVE_LEN          # ellipse centre (Y) = tangent point with the flat rim
    cz = H_RIM - FRONT_EZ                   # ellipse centre (Z)
    t_end = math.degrees(math.acos(-FRONT_CURVE_LEN / FRONT_EY))
    return (
        cq.Workplane("YZ")
        .moveTo(y_front, -1.0)
        .lineTo(y_back, -1.0)
        .lineTo(y_back, H_LID)
        .lineTo(y_lid, H_LID)
        .lineTo(y_lid - LID_CHAMFER, H_RIM)
        .lineTo(cy, H_RIM)
        .ellipseArc(FRONT_EY, FRONT_EZ, 90.0, t_end, sense=1, startAtCurrent=True)
        .close()
        .extrude(W + 10.0, both=True)
    )


# ---------------- outer body ----------------
outer = footprint(W, L, R_FRONT_CORNER, R_BACK_CORNER, H_LID + 5.0)
outer = outer.edges("<Z").fillet(R_BOTTOM)
outer = outer.intersect(side_profile())

# ---------------- cavity (open top, closed by the rear lid) ----------------
cav = footprint(W - 2 * T_WALL, L - 2 * T_WALL, R_FRONT_CORNER - T_WALL,
                R_BACK_INNER, 60.0, z0=T_FLOOR)
lid_block = (
    cq.Workplane("XY")
    .box(W + 10, y_back + 5 - y_lid, LID_T + 10, centered=(True, False, False))
    .translate((0, y_lid, H_LID - LID_T))
)
cav = cav.cut(lid_block)
body = outer.cut(cav)


# ---------------- round over the top edges of the rim, ramp and lid ----------------
def round_rim(b, r):
    s = b.val()
    tops = [f for f in s.Faces() if f.BoundingBox().zmin > H_FRONT - 1.0 and f.normalAt(f.Center()).z > 0.5]
    count = {}
    edges = {}
    for f in tops:
        for e in f.Edges():
            h = e.hashCode()
            count[h] = count.get(h, 0) + 1
            edges[h] = e
    sel = []
    for h, e in edges.items():
        bb = e.BoundingBox()
        if count[h] != 1:
            continue
        if abs(bb.ymin - y_lid) < 1e-3 and abs(bb.ymax - y_lid) < 1e-3:
            continue  # inner front edge of the lid stays sharp
        sel.append(e)
    return cq.Workplane().add(s.fillet(r, sel))


try:
    body = round_rim(body, RIM_ROUND)
except Exception as e:
    print("rim rounding skipped:", e)

# ---------------- raised floor under the lid ----------------
plat = (
    cq.Workplane("XY")
    .box(W - 2 * T_WALL, y_back - T_WALL - y_lid, PLATFORM_H, centered=(True, False, False))
    .edges("|Z and >Y").fillet(R_BACK_INNER - 0.01)
    .translate((0, y_lid, T_FLOOR - 0.01))
)
body = body.union(plat)

# ---------------- guide ribs on both inner side walls ----------------
z_r0 = T_FLOOR + PLATFORM_H - 0.1
z_r1 = H_LID - LID_T + 0.1
for dy in RIB_Y_FROM_LIDFRONT:
    yc = y_lid + dy
    for sx in (-1, 1):
        xc = sx * (W / 2.0 - T_WALL - RIB_D / 2.0 + 0.05)
        rib = (
            cq.Workplane("XY")
            .box(RIB_D + 0.1, RIB_W, z_r1 - z_r0, centered=(True, True, False))
            .translate((xc, yc, z_r0))
        )
        body = body.union(rib)

# ---------------- slotted screw bosses with countersunk slots ----------------
for (bx, by) in BOSSES:
    boss = (
        cq.Workplane("XY").workplane(offset=T_FLOOR - 0.1)
        .center(bx, by).slot2D(BOSS_LEN, BOSS_W, 90).extrude(BOSS_H + 0.1)
    )
    body = body.union(boss)
    slot = (
        cq.Workplane("XY").workplane(offset=-1.0)
        .center(bx, by).slot2D(SLOT_LEN, SLOT_W, 90).extrude(T_FLOOR + BOSS_H + 3.0)
    )
    csk_h = (CSK_W - SLOT_W) / 2.0
    csk = (
        cq.Workplane("XY").workplane(offset=-0.01)
        .center(bx, by).slot2D(CSK_LEN, CSK_W, 90)
        .workplane(offset=csk_h + 0.01).slot2D(SLOT_LEN, SLOT_W, 90)
        .loft()
    )
    body = body.cut(slot).cut(csk)

# ---------------- front windows ----------------
for (x0, x1, z0, z1) in WINDOWS:
    win = (
        cq.Workplane("XY").box(x1 - x0, 4 * T_WALL + 4, z1 - z0, centered=False)
        .translate((x0, y_front - 2 - T_WALL, z0))
    )
    body = body.cut(win)


# ---------------- lettering ----------------
def scaled_text(txt, length, height, depth, font=FONT):
    from OCP.gp import gp_GTrsf, gp_Mat, gp_XYZ
    from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform
    t = cq.Workplane("XY").text(txt, 20.0, depth, fontPath=font, halign="center", valign="bottom")
    s = t.val()
    bb = s.BoundingBox()
    sx = length / (bb.xmax - bb.xmin)
    sy = height / (bb.ymax - bb.ymin)
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(sx, 0, 0, 0, sy, 0, 0, 0, 1))
    g.SetTranslationPart(gp_XYZ(-0.5 * (bb.xmin + bb.xmax) * sx, -bb.ymin * sy, 0))
    return cq.Shape.cast(BRepBuilderAPI_GTransform(s.wrapped, g, True).Shape())


try:
    # +X side: reads front -> back
    txt1 = scaled_text(TEXT, TEXT_LEN, TEXT_H, TEXT_DEPTH + 0.2)
    pl1 = cq.Plane(origin=(W / 2.0 - 0.2, TEXT_YC, TEXT_BASE_Z), xDir=(0, 1, 0), normal=(1, 0, 0))
    body = body.union(cq.Workplane().add(txt1.moved(cq.Location(pl1))))
    # -X side: reads back -> front (slightly taller lettering on this side)
    txt2 = scaled_text(TEXT, TEXT_LEN, TEXT_H_LEFT, TEXT_DEPTH + 0.2)
    pl2 = cq.Plane(origin=(-W / 2.0 + 0.2, TEXT_YC, TEXT_BASE_Z_LEFT), xDir=(0, -1, 0), normal=(-1, 0, 0))
    body = body.union(cq.Workplane().add(txt2.moved(cq.Location(pl2))))
except Exception as e:  # lettering is decorative; keep the body if fonts are missing
    print("lettering skipped:", e)


# ---------------- rear logo: stylised serif "X" whose upper arm is three dots ----------------
# face coordinates on the back face: u = -X (reads left->right seen from behind), v = Z
LOGO_THIN = ((-4.0, 21.6), (4.3, 9.0), 0.9)            # thin stroke ends + width
LOGO_THIN_SERIFS = (((-8.9, 22.1), (-3.3, 22.3), (-4.6, 20.3)),
                    ((2.6, 7.4), (7.2, 7.4), (4.9, 9.7)))
LOGO_THICK = ((-7.6, 7.4), (-4.1, 7.4), (1.6, 15.9), (-1.9, 16.1))
LOGO_THICK_SERIF = ((-9.2, 7.4), (-3.0, 7.4), (-3.9, 8.5), (-8.1, 8.5))
LOGO_DOTS = ((1.3, 18.8), (3.6, 21.8), (5.9, 24.9))
LOGO_DOT = (3.2, 1.6)
LOGO_OFFSET = (0.8, 0.3)


def logo_solid():
    h = LOGO_DEPTH + 0.2
    wp = cq.Workplane("XY")
    (a, b, w) = LOGO_THIN
    dx, dy = b[0] - a[0], b[1] - a[1]
    n = math.hypot(dx, dy)
    nx, ny = -dy / n * w / 2, dx / n * w / 2
    s = wp.polyline([(a[0] + nx, a[1] + ny), (b[0] + nx, b[1] + ny),
                     (b[0] - nx, b[1] - ny), (a[0] - nx, a[1] - ny)]).close().extrude(h)
    for tri in LOGO_THIN_SERIFS:
        s = s.union(wp.polyline(list(tri)).close().extrude(h))
    s = s.union(wp.polyline(list(LOGO_THICK)).close().extrude(h))
    s = s.union(wp.polyline(list(LOGO_THICK_SERIF)).close().extrude(h))
    (c0, c1) = LOGO_DOTS[0], LOGO_DOTS[-1]
    ang = math.degrees(math.atan2(c1[1] - c0[1], c1[0] - c0[0])) + 90.0
    for (px, py) in LOGO_DOTS:
        s = s.union(cq.Workplane("XY").center(px, py).slot2D(LOGO_DOT[0], LOGO_DOT[1], ang).extrude(h))
    return s.val()


try:
    lg = logo_solid()
    pl3 = cq.Plane(origin=(-LOGO_OFFSET[0], y_back - 0.2, LOGO_OFFSET[1]), xDir=(-1, 0, 0), normal=(0, 1, 0))
    body = body.union(cq.Workplane().add(lg.moved(cq.Location(pl3))))
except Exception as e:
    print("logo skipped:", e)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
